import math
import cadquery as cq

# Phone stand with a 5-hole pen rack in the front lip, a slanted rest rising out of a
# round groove, and a hollow triangular support open on both sides.
VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- driving dimensions (mm) ----------------
W = 78.0          # overall width (X)
D = 74.9          # overall depth (Y)
T_BASE = 4.0      # base plate thickness
T_BACK = 3.8      # back wall thickness
T_SLANT = 3.5     # slanted (phone rest) plate thickness
SLANT_DEG = 20.0  # slanted plate angle from vertical

LIP_H = 19.6      # height of front lip
GROOVE_R = 9.5    # radius of the groove at the bottom of the rest
GROOVE_Y = 26.0   # groove centre, distance from front face
GROOVE_Z = 16.25  # groove centre height

EDGE_R = 1.0      # rounding of all outer edges except the base

N_HOLES = 5
HOLE_D = 12.4
HOLE_PITCH = 14.8
HOLE_Y = 8.6      # hole centre distance from front face
HOLE_X_OFF = 0.45 # small sideways offset of the hole row (+X)
HOLE_DEPTH = LIP_H - T_BASE   # blind, floor as thick as the base

# ---------------- derived geometry ----------------
a = math.radians(SLANT_DEG)
u = (math.sin(a), math.cos(a))        # direction along the plate (up/back)
n = (math.cos(a), -math.sin(a))       # normal pointing to back side

# tangent point of slanted front face on the groove circle
Tp = (GROOVE_Y + GROOVE_R * n[0], GROOVE_Z + GROOVE_R * n[1])
# front face meets back face
s_top = (D - Tp[0]) / u[0]
Z_TOP = Tp[1] + s_top * u[1]

# back face of the slanted plate
Bp = (Tp[0] + T_SLANT * n[0], Tp[1] + T_SLANT * n[1])
s_b = (T_BASE - Bp[1]) / u[1]
tri_y0 = Bp[0] + s_b * u[0]
s_i = (D - T_BACK - Bp[0]) / u[0]
tri_z1 = Bp[1] + s_i * u[1]

am = math.radians(-100.0)
arc_mid = (GROOVE_Y + GROOVE_R * math.cos(am), GROOVE_Z + GROOVE_R * math.sin(am))
left_pt = (GROOVE_Y - GROOVE_R, GROOVE_Z)

# ---------------- side profile (YZ plane), extruded along X ----------------
prism = (
    cq.Workplane("YZ")
    .moveTo(0, 0)
    .lineTo(D, 0)
    .lineTo(D, Z_TOP)
    .lineTo(Tp[0], Tp[1])
    .threePointArc(arc_mid, left_pt)
    .lineTo(left_pt[0], LIP_H)
    .lineTo(0, LIP_H)
    .close()
    .extrude(W / 2.0, both=True)
)


def _keep(e):
    bb = e.BoundingBox()
    if bb.zmax < 1e-6:                      # edges of the base: stay sharp
        return False
    if bb.xlen > 0.9 * W:                   # X-parallel edges: skip the tangent ones
        c = e.Center()
        for p in (left_pt, Tp):
            if abs(c.y - p[0]) < 1e-3 and abs(c.z - p[1]) < 1e-3:
                return False
    return True


prism = prism.newObject([e for e in prism.edges().vals() if _keep(e)]).fillet(EDGE_R)

# triangular through-opening under the rest
tri = (
    cq.Workplane("YZ")
    .polyline([(tri_y0, T_BASE), (D - T_BACK, T_BASE), (D - T_BACK, tri_z1)])
    .close()
    .extrude(W, both=True)
)
body = prism.cut(tri)

# pen holes in the lip
xs = [HOLE_X_OFF + (i - (N_HOLES - 1) / 2.0) * HOLE_PITCH for i in range(N_HOLES)]
holes = (
    cq.Workplane("XY")
    .workplane(offset=LIP_H - HOLE_DEPTH)
    .pushPoints([(x, HOLE_Y) for x in xs])
    .circle(HOLE_D / 2.0)
    .extrude(HOLE_DEPTH + 1.0)
)
body = body.cut(holes)

result = body
